import math
import numpy as np
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.BRepAdaptor import BRepAdaptor_Curve
from OCP.TColgp import TColgp_Array1OfPnt2d
from OCP.gp import gp_Pnt2d

# ---------------- driving dimensions (mm) ----------------
# palm: slab between the palmar (-X) and dorsal (+X) faces, outline in the YZ plane
X_BACK = 14.0        # dorsal (+X) face of the palm
X_FRONT = -11.6      # palmar (-X) face of the palm at the knuckles
# palmar face profile in the XZ plane (x, z): bulges below the knuckles
FRONT_PROFILE = [(-13.0, -12.0), (-13.0, 0.0), (-14.8, 10.0), (-15.8, 25.0),
                 (-15.6, 40.0), (-14.8, 52.0), (-13.6, 60.0), (-12.2, 67.0),
                 (-11.6, 74.0), (-11.6, 110.0)]
# variable rounding of the dorsal / palmar perimeter: (y, z, radius) stations
# (full round along the little-finger side, tighter over the knuckles)
R_BACK = [(26.3, -12.0, 12.5), (45.0, 60.0, 12.5), (44.5, 72.0, 12.0), (36.0, 82.0, 10.0),
          (18.0, 90.5, 9.0), (-15.0, 94.4, 9.0), (-22.0, 92.0, 9.0), (-28.0, 80.0, 11.0),
          (-34.0, 55.0, 12.5), (-25.0, -12.0, 12.5)]
R_FRONT = [(26.3, -12.0, 12.0), (45.0, 60.0, 12.0), (44.5, 72.0, 11.0), (36.0, 82.0, 8.0),
           (18.0, 90.5, 4.5), (-15.0, 94.4, 4.5), (-22.0, 92.0, 5.5), (-28.0, 80.0, 9.0),
           (-34.0, 55.0, 12.0), (-25.0, -12.0, 12.0)]
R_WRIST = 3.0        # (below the wrist plane, trimmed away)

# right-view (Y,Z) outline of the palm, counter-clockwise from the wrist
PALM_OUTLINE = [
    (26.4, 4.0), (28.8, 9.6), (32.0, 16.0), (35.2, 24.0),
    (38.2, 32.0), (40.8, 40.0), (43.2, 48.0), (44.7, 56.0), (45.3, 64.0),
    (44.8, 71.0), (42.5, 76.0), (36.0, 82.0), (28.0, 86.2), (18.0, 90.3),
    (8.0, 92.5), (-4.0, 93.4), (-12.0, 94.2), (-19.0, 93.9), (-23.5, 91.0),
    (-26.6, 85.0),
    (-28.5, 79.0), (-31.5, 69.0), (-34.0, 59.0), (-35.0, 48.0),
    (-33.5, 36.0), (-30.5, 24.0), (-27.5, 13.0), (-25.6, 4.0),
]
Y_WRIST = (-25.0, 26.3)   # wrist width (Y) at z = 0
Z_SUB = -20.0             # outline is extended below the wrist, trimmed at z = 0

# finger slots (index -> little finger)
SLOT_Y = [-14.0, 2.9, 19.8, 36.2]      # slot centres along Y
SLOT_W = 13.8                          # slot width
SLOT_ZB = [86.2, 82.9, 78.3, 69.7]     # slot floor height (through cut)
SLOT_R = 2.5                           # floor corner radius
PIN_X = 2.9                            # knuckle pin axis X
PIN_DZ = 2.5                           # pin axis below the slot floor
PIN_D = 4.0                            # knuckle pin diameter
CRADLE_R = 6.0                         # cylindrical cradle around the pin
RAMP_X0 = -3.0                         # palmar ramp starts here on the slot floor
RAMP_DROP = 9.0                        # ramp drop at the palmar face
TENDON_D = 2.0                         # tendon hole in the ramp

# thumb end face (mounting face for the thumb)
THUMB_C = (-35.7, -37.3, 45.9)         # centre of the end face
THUMB_N = (-0.55, -0.10, 0.83)         # outward normal
THUMB_U = (0.67, -0.52, 0.45)          # long axis of the face
THUMB_L = 20.0
THUMB_W = 9.0
THUMB_TIP_R = 3.5
THUMB_CAP_S = 0.6                      # beyond the face the lobe closes to this scale
THUMB_CAP_H = 4.0                      # ... at this distance past the face plane
# neck section where the thumb leaves the palm surface, corners (X,Y,Z)
# matching the tip corners D (outer-low), C (outer-back), B (web-back), A (web-front)
THUMB_NECK = [(-12.5, -13.0, 1.0), (3.0, -24.5, 1.0), (9.0, -32.0, 47.0), (-14.0, 1.0, 44.0)]
THUMB_NECK_R = [5.0, 9.0, 11.0, 11.0]
THUMB_ROOT_S = 0.55                    # buried planar root: shrunken neck ...
THUMB_SINK = (7.0, 3.0, 0.0)           # ... pushed into the palm
THUMB_MID_T = 0.5                      # position of the inflated middle section
THUMB_MID_S = 1.03                     # inflation of the middle section
THUMB_MID_R = [6.0, 11.5, 11.5, 11.0]

# thumb mounting details
THUMB_SLOT_W = 2.2   # hinge slot in the thumb end face
THUMB_SLOT_L = 16.0
THUMB_SLOT_D = 4.0
THUMB_SLOT_OFF = 2.2  # slot offset from the +v edge of the face
THUMB_HOLE = (-29.6, -29.0, 2.6)   # vertical pin hole in the top of the thumb (x, y, d)

# wrist
NOTCH_W = 17.2       # dorsal wrist notch width (Y)
NOTCH_H = 8.5        # height
NOTCH_D = 5.0        # depth (X)
FNOTCH_W = 14.0      # palmar wrist recess
FNOTCH_H = 6.0
FNOTCH_D = 2.5
# wrist mounting holes (x, y, diameter, depth)
WRIST_HOLES = [(0.5, -21.3, 4.2, 10.0), (0.5, 21.3, 4.2, 10.0),
               (-1.6, -16.0, 3.4, 6.0), (-1.6, 16.0, 3.4, 6.0),
               (3.0, 0.0, 1.5, 5.0), (6.0, 0.0, 1.5, 5.0), (0.0, 0.0, 1.5, 5.0),
               (3.0, 3.0, 1.5, 5.0), (3.0, -3.0, 1.5, 5.0)]


def V(t):
    return cq.Vector(*t)


def param_near(edge, y, z, n=2000):
    """parameter of the point of an edge closest to (y, z) in the YZ projection"""
    c = BRepAdaptor_Curve(edge.wrapped)
    u0, u1 = c.FirstParameter(), c.LastParameter()
    best = None
    for i in range(n + 1):
        u = u0 + (u1 - u0) * i / n
        p = c.Value(u)
        d = (p.Y() - y) ** 2 + (p.Z() - z) ** 2
        if best is None or d < best[0]:
            best = (d, u)
    return best[1]


def perimeter_fillet(shape, face, stations, r_const):
    """variable-radius fillet of the boundary of a face: the long (outline) edge
    gets the radius law given by the stations, the short wrist edge a constant"""
    mf = BRepFilletAPI_MakeFillet(shape.wrapped)
    for e in face.Edges():
        if e.geomType() == "LINE":
            mf.Add(float(r_const), e.wrapped)
        else:
            pairs = sorted((param_near(e, y, z), r) for (y, z, r) in stations)
            arr = TColgp_Array1OfPnt2d(1, len(pairs))
            for i, (u, r) in enumerate(pairs):
                arr.SetValue(i + 1, gp_Pnt2d(u, r))
            mf.Add(arr, e.wrapped)
    mf.Build()
    return cq.Workplane("XY").add(cq.Shape.cast(mf.Shape()))


# ---------------- palm slab ----------------
y_neg, y_pos = Y_WRIST
pts = ([cq.Vector(0, y_pos, Z_SUB), cq.Vector(0, y_pos, Z_SUB / 2)]
       + [cq.Vector(0, y, z) for (y, z) in PALM_OUTLINE]
       + [cq.Vector(0, y_neg, Z_SUB / 2), cq.Vector(0, y_neg, Z_SUB)])
spl = cq.Edge.makeSpline(pts)
bottom = cq.Edge.makeLine(cq.Vector(0, y_neg, Z_SUB), cq.Vector(0, y_pos, Z_SUB))
outline = cq.Wire.assembleEdges([spl, bottom])
X_SLAB0 = -20.0
slab = cq.Solid.extrudeLinear(cq.Face.makeFromWires(outline),
                              cq.Vector(X_BACK - X_SLAB0, 0, 0))
slab = slab.translate(cq.Vector(X_SLAB0, 0, 0))
palm = perimeter_fillet(slab, cq.Workplane("XY").add(slab).faces(">X").val(), R_BACK, R_WRIST)
# palmar side: prism of the XZ front profile, extruded along Y
fp = [cq.Vector(x, 0, z) for (x, z) in FRONT_PROFILE]
fw = cq.Wire.assembleEdges([
    cq.Edge.makeSpline(fp),
    cq.Edge.makeLine(fp[-1], cq.Vector(30, 0, fp[-1].z)),
    cq.Edge.makeLine(cq.Vector(30, 0, fp[-1].z), cq.Vector(30, 0, fp[0].z)),
    cq.Edge.makeLine(cq.Vector(30, 0, fp[0].z), fp[0]),
])
prism = cq.Solid.extrudeLinear(cq.Face.makeFromWires(fw), cq.Vector(0, 120, 0))
prism = prism.translate(cq.Vector(0, -60, 0))
palm = palm.intersect(cq.Workplane("XY").add(prism))
palm = perimeter_fillet(palm.val(), palm.faces("<X").val(), R_FRONT, R_WRIST)


# ---------------- thumb ----------------
def rounded_poly(corners, r):
    """closed wire through corner points with circular corner blends;
    the first edge always starts just after corner 0 (deterministic for lofts)"""
    P = [V(c) for c in corners]
    n = len(P)
    radii = r if isinstance(r, (list, tuple)) else [r] * n
    tin, tout, mids = [], [], []
    for i in range(n):
        r = radii[i]
        a = (P[i - 1] - P[i]).normalized()
        b = (P[(i + 1) % n] - P[i]).normalized()
        half = math.acos(max(-1.0, min(1.0, a.dot(b)))) / 2.0
        d = r / math.tan(half)
        bis = (a + b).normalized()
        ctr = P[i] + bis * (r / math.sin(half))
        tin.append(P[i] + a * d)
        tout.append(P[i] + b * d)
        mids.append(ctr - bis * r)
    edges = []
    for i in range(n):
        j = (i + 1) % n
        edges.append(cq.Edge.makeLine(tout[i], tin[j]))
        edges.append(cq.Edge.makeThreePointArc(tin[j], mids[j], tout[j]))
    return cq.Wire.assembleEdges(edges)


def face_frame(center, normal, udir):
    n = V(normal).normalized()
    u = V(udir)
    u = (u - n * u.dot(n)).normalized()
    v = n.cross(u)
    return V(center), n, u, v


def face_corners(center, normal, udir, L, W):
    c, n, u, v = face_frame(center, normal, udir)
    # order: D(-u,-v)  C(+u,-v)  B(+u,+v)  A(-u,+v)
    return [c + u * (sx * L / 2) + v * (sy * W / 2)
            for sx, sy in ((-1, -1), (1, -1), (1, 1), (-1, 1))]


tip_pts = face_corners(THUMB_C, THUMB_N, THUMB_U, THUMB_L, THUMB_W)
tip = rounded_poly(tip_pts, THUMB_TIP_R)
def planarize(points):
    """orthogonal projection of points onto their least-squares plane"""
    P = np.array(points, dtype=float)
    c = P.mean(axis=0)
    n = np.linalg.svd(P - c)[2][2]
    return [V(tuple(p - np.dot(p - c, n) * n)) for p in P]


neck_pts = [V(p) for p in THUMB_NECK]
neck = rounded_poly(neck_pts, THUMB_NECK_R)
ncen = sum(neck_pts, cq.Vector(0, 0, 0)) * (1.0 / len(neck_pts))
root_pts = planarize([(ncen + (p - ncen) * THUMB_ROOT_S + V(THUMB_SINK)).toTuple()
                      for p in neck_pts])
root = rounded_poly(root_pts, [r * THUMB_ROOT_S for r in THUMB_NECK_R])
# middle section: interpolated corners, inflated about the section centroid
mid_pts = [a + (b - a) * THUMB_MID_T for a, b in zip(neck_pts, tip_pts)]
cen = sum(mid_pts, cq.Vector(0, 0, 0)) * (1.0 / len(mid_pts))
mid_pts = [cen + (p - cen) * THUMB_MID_S for p in mid_pts]
mid = rounded_poly(mid_pts, THUMB_MID_R)
# closing section beyond the face: the lobe is rounded over and then trimmed
cap_c = V(THUMB_C) + V(THUMB_N).normalized() * THUMB_CAP_H
cap = rounded_poly(face_corners(cap_c.toTuple(), THUMB_N, THUMB_U,
                                THUMB_L * THUMB_CAP_S, THUMB_W * THUMB_CAP_S), THUMB_TIP_R * THUMB_CAP_S)
thumb = cq.Solid.makeLoft([root, neck, mid, tip, cap], False)
# trim flush with the mounting face
fc, fn, fu, fv = face_frame(THUMB_C, THUMB_N, THUMB_U)
trim = cq.Solid.makeBox(200, 200, 100).transformShape(
    cq.Plane(origin=fc - fu * 100 - fv * 100, xDir=fu, normal=fn).rG)
thumb = thumb.cut(trim)

body = palm.union(cq.Workplane("XY").add(thumb))
# trim at the wrist plane
body = body.intersect(cq.Workplane("XY").box(200, 200, 200, centered=(True, True, False)))

# ---------------- finger slots, cradles, ramps, pins ----------------
pins = []
for yc, zb in zip(SLOT_Y, SLOT_ZB):
    cut = (cq.Workplane("YZ").workplane(offset=-40)
           .center(yc, (zb + 110) / 2)
           .rect(SLOT_W, 110 - zb).extrude(80))
    cut = cut.edges("|X").edges("<Z").fillet(SLOT_R)
    body = body.cut(cut)
    zp = zb - PIN_DZ
    cradle = (cq.Workplane("XZ", origin=(0, yc + SLOT_W / 2, 0))
              .center(PIN_X, zp).circle(CRADLE_R).extrude(SLOT_W))
    body = body.cut(cradle)
    # palmar ramp towards the tendon exit
    ramp = (cq.Workplane("XZ", origin=(0, yc + SLOT_W / 2, 0))
            .polyline([(RAMP_X0, zb + 0.01), (X_FRONT - 6, zb + 0.01),
                       (X_FRONT - 6, zb - RAMP_DROP - 6 * RAMP_DROP / (RAMP_X0 - X_FRONT)),
                       ]).close().extrude(SLOT_W))
    body = body.cut(ramp)
    # tendon hole normal to the ramp
    xm = (RAMP_X0 + X_FRONT) / 2
    zm = zb - RAMP_DROP / 2
    ang = math.degrees(math.atan2(RAMP_DROP, RAMP_X0 - X_FRONT))
    hole = (cq.Workplane("XZ", origin=(0, yc, 0))
            .transformed(offset=(xm, zm, 0), rotate=(0, 0, 0))
            )
    d = cq.Vector(math.sin(math.radians(ang)), 0, -math.cos(math.radians(ang)))
    h = cq.Solid.makeCylinder(TENDON_D / 2, 14, cq.Vector(xm, yc, zm) - d * 1.0, d)
    body = body.cut(cq.Workplane("XY").add(h))
    pins.append(cq.Solid.makeCylinder(PIN_D / 2, SLOT_W + 1.0,
                                      cq.Vector(PIN_X, yc - SLOT_W / 2 - 0.5, zp),
                                      cq.Vector(0, 1, 0)))
for p in pins:
    body = body.union(cq.Workplane("XY").add(p))

# ---------------- thumb mounting face details ----------------
c, n, u, v = face_frame(THUMB_C, THUMB_N, THUMB_U)
sc = c + v * (THUMB_W / 2 - THUMB_SLOT_OFF)
slot_box = cq.Solid.makeBox(THUMB_SLOT_L, THUMB_SLOT_W, THUMB_SLOT_D + 2)
pl = cq.Plane(origin=sc - u * (THUMB_SLOT_L / 2) - v * (THUMB_SLOT_W / 2) - n * THUMB_SLOT_D,
              xDir=u, normal=n)
slot_box = slot_box.transformShape(pl.rG)
body = body.cut(cq.Workplane("XY").add(slot_box))
body = body.cut(cq.Workplane("XY").add(cq.Solid.makeCylinder(
    THUMB_HOLE[2] / 2, 25.0, cq.Vector(THUMB_HOLE[0], THUMB_HOLE[1], 36.0), cq.Vector(0, 0, 1))))

# ---------------- wrist ----------------
notch = cq.Workplane("XY").box(NOTCH_D + 10, NOTCH_W, NOTCH_H, centered=(False, True, False)) \
    .translate((X_BACK - NOTCH_D, 0, 0))
body = body.cut(notch)
fnotch = cq.Workplane("XY").box(FNOTCH_D + 10, FNOTCH_W, FNOTCH_H, centered=(False, True, False)) \
    .translate((X_FRONT - 1.2 - 10, 0, 0))
body = body.cut(fnotch)
for (hx, hy, hd, hdep) in WRIST_HOLES:
    body = body.cut(cq.Workplane("XY").add(
        cq.Solid.makeCylinder(hd / 2, hdep, cq.Vector(hx, hy, -0.1), cq.Vector(0, 0, 1))))

result = body
